import math
import cadquery as cq

# ---------------------------------------------------------------
# Ultrasonic distance sensor module (HC-SR04 style)
# PCB lies in the XZ plane, front (component) face at Y = 0 facing -Y,
# transducers and crystal on the back face (+Y side).
# ---------------------------------------------------------------

# PCB
PCB_W = 45.0          # along X
PCB_H = 20.5          # along Z
PCB_T = 1.6           # along Y
PCB_CORNER_R = 0.5
HOLE_D = 2.2
HOLE_INSET = 1.5     # hole centre from PCB edges

# Transducers
TR_D = 15.9
TR_L = 11.7            # to the rim (disc adds TR_DISC_H)
TR_X = 13.0           # +/- X position of transducer axes
TR_Z = 0.0
TR_TAPER = 0.15        # radius reduction over the length (slight draft)
TR_FILLET = 0.45       # small round on the outer rim
TR_DISC_D = 13.2       # raised membrane disc on the end face
TR_DISC_H = 0.2
TR_SEAM_ROT = 130.0    # rotate the cylinder about its axis (puts the seam out of sight)

# Crystal (HC-49 style, on the back face)
XT_L = 10.2           # length along X
XT_W = 3.8            # width along Z
XT_H = 2.95           # body height along Y
XT_TOP_Z = 9.48       # top of the body
XT_FLANGE = 0.25      # flange overhang
XT_FLANGE_T = 0.48
XT_FILLET = 0.3
XT_CORNER_R = 1.3      # rounded-rectangle outline of the can

# SOIC chips (front face)
IC_L = 10.2
IC_W = 4.0
IC_T = 0.5
IC_X = 12.5
IC_PINS = 7
IC_PITCH = 1.27
LEAD_W = 0.22
LEAD_L = 1.0
LEAD_T = 0.2

# SMD passives (front face)
SMD_L = 1.2
SMD_W = 0.45
SMD_W2 = 0.55
SMD_T = 0.32

# Pin header (right-angle, 4 pins)
HDR_N = 4
HDR_PITCH = 2.54
HDR_DEPTH = 2.5       # along -Y
HDR_H = 2.62          # body height (Z)
HDR_CH = 0.45         # corner chamfer of each unit
HDR_BOTTOM_GAP = 0.1  # header bottom above PCB bottom edge
PIN_S = 0.5           # square pin section
PIN_BEND_R = 1.35     # centre-line bend radius
PIN_OUT = 1.95        # vertical leg centre distance from header face
PIN_BELOW = 2.5       # tip below PCB bottom edge
PIN_BACK = 1.25       # protrusion behind PCB (solder cone + tip)
SOLDER_R1 = 0.45      # solder cone base radius
SOLDER_R2 = 0.2       # solder cone top radius
TIP_L = 0.3           # pointed pin tip length

# ---------------------------------------------------------------
# PCB with mounting holes
# ---------------------------------------------------------------
hx = PCB_W / 2 - HOLE_INSET
hz = PCB_H / 2 - HOLE_INSET
pcb = (
    cq.Workplane("XZ")
    .rect(PCB_W, PCB_H)
    .extrude(-PCB_T)                      # XZ normal is -Y, so -T goes to +Y
    .edges("|Y").fillet(PCB_CORNER_R)
    .faces("<Y").workplane()
    .pushPoints([(hx, hz), (-hx, hz), (hx, -hz), (-hx, -hz)])
    .hole(HOLE_D)
)
result = pcb

# ---------------------------------------------------------------
# Transducers
# ---------------------------------------------------------------
def transducer():
    # slightly tapered can (end radius TR_TAPER smaller than the base)
    taper_deg = math.degrees(math.atan(TR_TAPER / TR_L))
    plane = cq.Plane(origin=(0, 0, 0), xDir=(1, 0, 0), normal=(0, 1, 0))
    body = (
        cq.Workplane(plane)
        .circle(TR_D / 2)
        .extrude(TR_L, taper=taper_deg)   # along +Y
        .faces(">Y").edges().fillet(TR_FILLET)
    )
    disc_plane = cq.Plane(origin=(0, TR_L, 0), xDir=(1, 0, 0), normal=(0, 1, 0))
    disc = (
        cq.Workplane(disc_plane)
        .circle(TR_DISC_D / 2)
        .extrude(TR_DISC_H)
    )
    return body.union(disc).rotate((0, 0, 0), (0, 1, 0), TR_SEAM_ROT)


for sx in (-1, 1):
    tr = transducer().translate((sx * TR_X, PCB_T, TR_Z))
    result = result.union(tr)

# ---------------------------------------------------------------
# Crystal on the back face
# ---------------------------------------------------------------
xt_zc = XT_TOP_Z - XT_W / 2
flange = (
    cq.Workplane("XZ", origin=(0, PCB_T, 0))
    .center(0, xt_zc)
    .rect(XT_L + 2 * XT_FLANGE, XT_W + 2 * XT_FLANGE)
    .extrude(-XT_FLANGE_T)
    .edges("|Y").fillet(XT_CORNER_R + XT_FLANGE)
)
xtal = (
    cq.Workplane("XZ", origin=(0, PCB_T + XT_FLANGE_T, 0))
    .center(0, xt_zc)
    .rect(XT_L, XT_W)
    .extrude(-XT_H)
    .edges("|Y").fillet(XT_CORNER_R)
)
xtal = xtal.faces(">Y").edges().fillet(XT_FILLET)
result = result.union(flange).union(xtal)

# ---------------------------------------------------------------
# SOIC chips on the front face
# ---------------------------------------------------------------
def soic(xc, zc):
    body = (
        cq.Workplane("XY")
        .box(IC_L, IC_T, IC_W)
        .translate((xc, -IC_T / 2, zc))
        .edges("|Y").fillet(0.1)
    )
    span = (IC_PINS - 1) * IC_PITCH
    for i in range(IC_PINS):
        x = xc - span / 2 + i * IC_PITCH
        for sz in (-1, 1):
            lead = (
                cq.Workplane("XY")
                .box(LEAD_W, LEAD_T, LEAD_L + 0.5)
                .translate((x, -LEAD_T / 2, zc + sz * (IC_W / 2 + LEAD_L / 2 - 0.25)))
            )
            body = body.union(lead)
    return body


for sx in (-1, 1):
    result = result.union(soic(sx * IC_X, 0.0))

# ---------------------------------------------------------------
# SMD passives on the front face: (x, z, length, width)
# ---------------------------------------------------------------
SMDS = [
    # top-left row
    (-15.4, 7.54, SMD_L, SMD_W), (-13.8, 7.54, SMD_L, SMD_W), (-11.9, 7.54, SMD_L, SMD_W),
    # top centre pair
    (-2.72, 4.41, SMD_L, SMD_W2), (-1.13, 4.41, SMD_L, SMD_W2),
    # top-right group
    (9.95, 7.54, 1.1, SMD_W), (11.84, 7.54, 2.05, SMD_W),
    (8.12, 6.21, SMD_L, SMD_W),
    (14.96, 5.06, SMD_L, SMD_W), (16.57, 5.06, SMD_L, SMD_W),
    # centre pair
    (-3.89, -2.67, 1.1, 0.4), (-4.86, -3.58, SMD_L, SMD_W2),
    # bottom-left row
    (-15.8, -6.2, SMD_L, SMD_W2), (-14.1, -6.2, SMD_L, SMD_W2), (-12.3, -6.2, SMD_L, SMD_W2),
    (-10.5, -6.2, SMD_L, SMD_W2), (-8.9, -6.2, SMD_L, SMD_W2),
    # bottom-right group
    (8.12, -5.59, SMD_L, SMD_W), (8.12, -7.43, SMD_L, SMD_W),
    (11.84, -7.43, SMD_L, SMD_W), (13.82, -7.43, SMD_L, SMD_W),
    (15.19, -7.43, SMD_L, SMD_W), (16.57, -7.43, SMD_L, SMD_W),
]

for (x, z, l, w) in SMDS:
    smd = (
        cq.Workplane("XY")
        .box(l, SMD_T, w)
        .translate((x, -SMD_T / 2, z))
        .edges("not <Y").fillet(0.08)
    )
    result = result.union(smd)

# ---------------------------------------------------------------
# Right-angle pin header at the bottom centre
# ---------------------------------------------------------------
hdr_zc = -PCB_H / 2 + HDR_BOTTOM_GAP + HDR_H / 2
uw = HDR_PITCH / 2
uh = HDR_H / 2
c = HDR_CH
oct_pts = [
    (-uw + c, -uh), (uw - c, -uh), (uw, -uh + c), (uw, uh - c),
    (uw - c, uh), (-uw + c, uh), (-uw, uh - c), (-uw, -uh + c),
]
span = (HDR_N - 1) * HDR_PITCH
pin_xs = [-span / 2 + i * HDR_PITCH for i in range(HDR_N)]

header = None
for x in pin_xs:
    u = (
        cq.Workplane("XZ", origin=(0, 0, 0))
        .center(x, hdr_zc)
        .polyline(oct_pts).close()
        .extrude(HDR_DEPTH)               # toward -Y
    )
    header = u if header is None else header.union(u)
result = result.union(header)

# pins
y_face = -HDR_DEPTH
y_vert = y_face - PIN_OUT                 # centre of vertical leg
y_bend = y_vert + PIN_BEND_R              # start of bend
z_bend = hdr_zc - PIN_BEND_R              # bend centre Z
z_tip = -PCB_H / 2 - PIN_BELOW

for x in pin_xs:
    # straight horizontal part (from behind the PCB to bend start)
    y0 = PCB_T + 0.3
    horiz = (
        cq.Workplane("XY")
        .box(PIN_S, y0 - y_bend, PIN_S)
        .translate((x, (y0 + y_bend) / 2, hdr_zc))
    )
    # bend: revolve the square section 90 deg about an axis parallel to X
    bend = (
        cq.Workplane("XZ", origin=(0, y_bend, 0))
        .center(x, hdr_zc)
        .rect(PIN_S, PIN_S)
        .revolve(90, (-x, -PIN_BEND_R, 0), (1 - x, -PIN_BEND_R, 0))
    )
    vert = (
        cq.Workplane("XY")
        .box(PIN_S, PIN_S, z_bend - z_tip)
        .translate((x, y_vert, (z_bend + z_tip) / 2))
        .faces("<Z").chamfer(0.15)
    )
    # solder cone + tip behind the PCB
    cone_h = PIN_BACK - TIP_L
    cone = cq.Workplane("XY").add(
        cq.Solid.makeCone(SOLDER_R1, SOLDER_R2, cone_h,
                          cq.Vector(x, PCB_T, hdr_zc), cq.Vector(0, 1, 0))
    )
    tip = cq.Workplane("XY").add(
        cq.Solid.makeCone(SOLDER_R2, 0.05, TIP_L,
                          cq.Vector(x, PCB_T + cone_h, hdr_zc), cq.Vector(0, 1, 0))
    )
    result = result.union(horiz).union(bend).union(vert).union(cone).union(tip)

VIEW = {"azimuth": 45, "elevation": 26}
